import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_TEETH = 16          # number of teeth
TIP_H = 22.5          # distance from the gear axis to the flat tooth tip
TIP_W = 2.05          # width of the flat tooth tip
R_ROOT = 16.5         # root circle radius
FLANK_DEG = 13.7      # flank angle measured from the tooth centre line
TOOTH_OFFSET = TIP_W / 2.0   # tooth centre line offset sideways (+Y) from the axis
LENGTH = 61.0         # face width (along X)
BORE_D = 12.3         # bore diameter
KEY_W = 4.1           # keyway width (double keyway, along Z)
KEY_SPAN = 20.5       # tip-to-tip length of the double keyway

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- single tooth (pointing +Z) ----------------
# Sketched on the YZ plane: local x = global Y, local y = global Z, extrude +X.
t = math.tan(math.radians(FLANK_DEG))
v_bot = R_ROOT - 1.5                      # flanks run a little below the root circle
drop = TIP_H - v_bot
c = TOOTH_OFFSET
tooth_profile = [
    (c - TIP_W / 2.0, TIP_H),
    (c + TIP_W / 2.0, TIP_H),
    (c + TIP_W / 2.0 + drop * t, v_bot),
    (c - TIP_W / 2.0 - drop * t, v_bot),
]
tooth = cq.Workplane("YZ").polyline(tooth_profile).close().extrude(LENGTH).val()

# ---------------- gear body ----------------
body = cq.Workplane("YZ").circle(R_ROOT).extrude(LENGTH)

# polar pattern of the tooth about the gear axis (X)
pitch = 360.0 / N_TEETH
teeth = [tooth.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), i * pitch)
         for i in range(N_TEETH)]
body = body.union(cq.Workplane("YZ").newObject(teeth))

# ---------------- bore with double keyway ----------------
bore = (
    cq.Workplane("YZ")
    .circle(BORE_D / 2.0)
    .extrude(LENGTH)
    .union(cq.Workplane("YZ").rect(KEY_W, KEY_SPAN).extrude(LENGTH))
)
body = body.cut(bore)

# centre the part along X
result = body.translate((-LENGTH / 2.0, 0, 0))
